import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 99.3           # overall width  (X)
D = 30.0           # overall depth  (Y)  front plate at -Y, open at +Y
H = 103.0          # overall height (Z)
T = 2.3            # outer wall thickness
TF = 2.3           # front plate thickness
TI = 2.2           # inner partition wall thickness
R_OUT = 2.5        # fillet on the four outer edges running along Y
R_CAV = 3.0        # corner radius of the cavity (vertical-in-Y corners)
R_FLOOR = 4.0      # fillet between cavity walls and the floor (front plate)

# inner compartment (lower +X corner, seen from the back)
COMP_X_WALL = -2.0     # X of the compartment's -X partition (centre of wall)
COMP_Z_WALL = 60.0     # Z of the compartment's top partition (centre of wall)

# slot in the top wall, open to the back edge
SLOT_X = -29.5
SLOT_W = 13.2
SLOT_LEN = 17.5        # from the back edge to the end of the round end
SLOT_ENTRY_R = 2.2

# round hole in the bottom wall
BHOLE_X = -29.5
BHOLE_Y = 4.0
BHOLE_D = 19.5

# rectangular slot in the bottom wall (inside the compartment)
BSLOT_X = 19.8
BSLOT_Y = -2.0
BSLOT_L = 37.5
BSLOT_W = 11.5
BSLOT_R = 2.5

# small holes through the front plate
FHOLE_D = 2.4       # width of the small front slots
FHOLE_H = 3.2       # height of the small front slots
FHOLE_Z = 49.8
FHOLE_X = [-41.5, -14.0]

# ---------------- body ----------------
y0 = -D / 2.0
y1 = D / 2.0
outer = (
    cq.Workplane("XY")
    .box(W, D, H, centered=(True, True, False))
    .edges("|Y")
    .fillet(R_OUT)
)

y_floor = y0 + TF
cav_len = y1 - y_floor + 1.0

# inner limits
xi0 = -W / 2 + T
xi1 = W / 2 - T
zi0 = T
zi1 = H - T

# compartment rectangle (inside the partitions)
cx0 = COMP_X_WALL + TI / 2.0
cx1 = xi1
cz0 = zi0
cz1 = COMP_Z_WALL - TI / 2.0

# L-shaped region outside the partitions
px = COMP_X_WALL - TI / 2.0   # -X face of the vertical partition
pz = COMP_Z_WALL + TI / 2.0   # top face of the horizontal partition


def cavity_tool(pts):
    # profile in XZ, extruded along +Y from the floor to beyond the back
    wp = cq.Workplane("XZ", origin=(0, y_floor, 0))
    tool = wp.polyline(pts).close().extrude(-cav_len)
    tool = tool.edges("|Y").fillet(R_CAV)
    tool = tool.faces("<Y").edges().fillet(R_FLOOR)
    return tool


L_pts = [
    (xi0, zi0),
    (px, zi0),
    (px, pz),
    (xi1, pz),
    (xi1, zi1),
    (xi0, zi1),
]
C_pts = [
    (cx0, cz0),
    (cx1, cz0),
    (cx1, cz1),
    (cx0, cz1),
]

body = outer.cut(cavity_tool(L_pts)).cut(cavity_tool(C_pts))

# ---------------- top slot (open to the back) ----------------
slot_end_c = y1 - SLOT_LEN + SLOT_W / 2.0
slot = (
    cq.Workplane("XY", origin=(0, 0, H - T - 1.0))
    .center(SLOT_X, (slot_end_c + y1 + 2.0) / 2.0)
    .rect(SLOT_W, (y1 + 2.0) - slot_end_c)
    .extrude(T + 2.0)
    .union(
        cq.Workplane("XY", origin=(0, 0, H - T - 1.0))
        .center(SLOT_X, slot_end_c)
        .circle(SLOT_W / 2.0)
        .extrude(T + 2.0)
    )
)
body = body.cut(slot)

# fillet the slot entry corners (vertical edges where slot meets back face)
def _entry_edges(e):
    c = e.Center()
    return (
        abs(c.y - y1) < 0.6
        and c.z > H - T - 0.1
        and abs(abs(c.x - SLOT_X) - SLOT_W / 2.0) < 0.2
    )

try:
    sel = [e for e in body.edges("|Z").vals() if _entry_edges(e)]
    if sel:
        body = body.newObject(sel).fillet(SLOT_ENTRY_R)
except Exception:
    pass

# ---------------- bottom round hole ----------------
bhole = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .center(BHOLE_X, BHOLE_Y)
    .circle(BHOLE_D / 2.0)
    .extrude(T + 2.0)
)
body = body.cut(bhole)

# ---------------- bottom rectangular slot ----------------
bslot = (
    cq.Workplane("XY", origin=(0, 0, -1.0))
    .center(BSLOT_X, BSLOT_Y)
    .rect(BSLOT_L, BSLOT_W)
    .extrude(T + 2.0)
    .edges("|Z")
    .fillet(BSLOT_R)
)
body = body.cut(bslot)

# ---------------- small front holes ----------------
for fx in FHOLE_X:
    h = (
        cq.Workplane("XZ", origin=(0, y0 + TF + 1.0, 0))
        .center(fx, FHOLE_Z)
        .slot2D(FHOLE_H, FHOLE_D, angle=90)
        .extrude(TF + 2.0)
    )
    body = body.cut(h)

result = body
